import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# Keycap lying on its back: open skirt faces -Y, keycap top face at +Y,
# cross stem (offset toward -X) sticking out of the skirt toward -Y.
W0 = 18.0      # skirt width (X) at the opening
H0 = 20.5      # skirt height (Z) at the opening
D = 13.75      # body depth (Y) from opening to top face
TAPER_X = 0.6  # inward taper of each side wall over the depth
RISE_Z = 1.66  # rise of the bottom (-Z) wall over the depth (top wall is flat)
RT0 = 1.05     # upper corner radius at opening
RB0 = 3.3      # lower corner radius at opening
RT1 = 1.05     # upper corner radius at top face
RB1 = 4.3      # lower corner radius at top face
TOP_CHAMFER = 0.4  # edge break on the keycap top face

T_WALL = 1.7   # skirt wall thickness
T_TOP = 1.5    # thickness of the keycap top (far wall)

STEM_D = 5.72      # stem outer diameter
STEM_X = -1.29     # stem offset in X from body centre
STEM_OUT = 5.14    # stem protrusion beyond the opening
CB_D = 5.35        # shallow counterbore in the stem end (cross arms end on it)
CB_DEPTH = 0.3
CROSS_W = 1.39     # cross arm width
CROSS_CH = 0.4     # entry chamfer of the cross
CROSS_DEPTH = 4.0  # depth of the cross socket

BOSS = 6.07        # square boss around stem root
BOSS_R = 0.2
RIB_Y0 = 6.3       # Y of the front face of the support ribs
BOSS_Y0 = 6.3      # Y of the front face of the square boss
RIB_TF = 1.66      # rib thickness at front
RIB_TB = 2.8       # rib thickness at root (draft)


def rrect(wp, w, zt, zb, rt, rb):
    """Closed wire: width w centred on x=0, top at zt, bottom at zb,
    upper corner radius rt (0 = sharp), lower corner radius rb."""
    hw = w / 2.0
    c = math.cos(math.pi / 4)
    s = wp.moveTo(-hw + rb, zb).lineTo(hw - rb, zb)
    s = s.threePointArc((hw - rb + rb * c, zb + rb - rb * c), (hw, zb + rb))
    if rt > 0:
        s = s.lineTo(hw, zt - rt)
        s = s.threePointArc((hw - rt + rt * c, zt - rt + rt * c), (hw - rt, zt))
        s = s.lineTo(-hw + rt, zt)
        s = s.threePointArc((-hw + rt - rt * c, zt - rt + rt * c), (-hw, zt - rt))
    else:
        s = s.lineTo(hw, zt)
        s = s.lineTo(-hw, zt)
    s = s.lineTo(-hw, zb + rb)
    s = s.threePointArc((-hw + rb - rb * c, zb + rb - rb * c), (-hw + rb, zb))
    return s.close()


def outer_at(y):
    f = y / D
    w = W0 - 2 * TAPER_X * f
    zt = H0 / 2
    zb = -H0 / 2 + RISE_Z * f
    rt = RT0 + (RT1 - RT0) * f
    rb = RB0 + (RB1 - RB0) * f
    return w, zt, zb, rt, rb


def inner_at(y):
    w, zt, zb, rt, rb = outer_at(y)
    return (w - 2 * T_WALL, zt - T_WALL, zb + T_WALL,
            max(rt - T_WALL, 0.0), rb - T_WALL)


# "XZ" workplane: local x -> X, local y -> Z, offset goes toward -Y
def loft_between(prof0, prof1, y0, y1):
    wp0 = cq.Workplane("XZ", origin=(0, y0, 0))
    s = rrect(wp0, *prof0)
    s = rrect(s.workplane(offset=-(y1 - y0)), *prof1)
    return s.loft(ruled=True)


# ---------------- outer body ----------------
body = loft_between(outer_at(0), outer_at(D), 0, D)
body = body.faces(">Y").edges().chamfer(TOP_CHAMFER)

# ---------------- cavity ----------------
YC = D - T_TOP  # inner ceiling
cavity = loft_between(inner_at(-0.5), inner_at(YC), -0.5, YC)
body = body.cut(cavity)

# ---------------- internal ribs / boss ----------------
ZC = 0.0  # stem axis height (centre of opening)
Y_ROOT = YC + 0.3  # rib / boss roots are sunk slightly into the keycap top


def rib_profile_xy(tf, tb):
    # trapezoid in a plane: front (small y) thickness tf, root thickness tb
    return [(-tf / 2, RIB_Y0), (tf / 2, RIB_Y0), (tb / 2, Y_ROOT), (-tb / 2, Y_ROOT)]


# vertical rib (plane thin in X), extruded along Z
vr = (cq.Workplane("XY", origin=(STEM_X, 0, -H0))
      .polyline(rib_profile_xy(RIB_TF, RIB_TB)).close()
      .extrude(2 * H0))
# horizontal rib (thin in Z), extruded along X
pts = [(y, z) for (z, y) in rib_profile_xy(RIB_TF, RIB_TB)]
hr = (cq.Workplane("YZ", origin=(-W0, 0, ZC))
      .polyline(pts).close()
      .extrude(2 * W0))
boss = (cq.Workplane("XZ", origin=(STEM_X, Y_ROOT, ZC))
        .rect(BOSS, BOSS).extrude(Y_ROOT - BOSS_Y0)
        .edges("|Y").fillet(BOSS_R))
ribs = vr.union(hr).union(boss).intersect(
    loft_between(inner_at(0), inner_at(YC + 0.01), 0, YC + 0.01))
body = body.union(ribs)

# ---------------- stem ----------------
# plane with x-axis toward -X so the cylinder seam sits on the hidden side
stem_pl = cq.Plane(origin=(STEM_X, BOSS_Y0 + 0.5, ZC), xDir=(-1, 0, 0), normal=(0, -1, 0))
stem = (cq.Workplane(stem_pl)
        .circle(STEM_D / 2).extrude(BOSS_Y0 + 0.5 + STEM_OUT))
body = body.union(stem)

# shallow counterbore in the stem end
y_end = -STEM_OUT
cb_pl = cq.Plane(origin=(STEM_X, y_end - 0.01, ZC), xDir=(-1, 0, 0), normal=(0, 1, 0))
cbore = cq.Workplane(cb_pl).circle(CB_D / 2).extrude(CB_DEPTH + 0.01)
body = body.cut(cbore)

# cross socket below the counterbore floor, arms clipped by the counterbore circle
y_fl = y_end + CB_DEPTH          # counterbore floor
xs_pl = cq.Plane(origin=(STEM_X, y_fl - 0.01, ZC), xDir=(1, 0, 0), normal=(0, 1, 0))
arm_h = cq.Workplane(xs_pl).rect(STEM_D, CROSS_W).extrude(CROSS_DEPTH)
arm_v = cq.Workplane(xs_pl).rect(CROSS_W, STEM_D).extrude(CROSS_DEPTH)
ch_h = (cq.Workplane(xs_pl).rect(STEM_D, CROSS_W + 2 * CROSS_CH)
        .workplane(offset=CROSS_CH + 0.01).rect(STEM_D, CROSS_W).loft())
ch_v = (cq.Workplane(xs_pl).rect(CROSS_W + 2 * CROSS_CH, STEM_D)
        .workplane(offset=CROSS_CH + 0.01).rect(CROSS_W, STEM_D).loft())
clip = cq.Workplane(cq.Plane(origin=(STEM_X, y_fl - 0.02, ZC), xDir=(-1, 0, 0), normal=(0, 1, 0))
                    ).circle(CB_D / 2).extrude(CROSS_DEPTH + 0.02)
cross = arm_h.union(arm_v).union(ch_h).union(ch_v).intersect(clip)
body = body.cut(cross)

result = body
